"""U-shaped (horseshoe) mounting block with an underside wiring channel.

Plan view: straight front face with a central U-slot, sides tapering inwards and a
rounded back (large arc blended into the sides by two fillets).  Top: four through
holes and one blind hole on the centre line.  Underside: a front pocket with a screw
boss in each prong, a wiring channel along each prong (separated from the slot by a
thin wall) and a ball-end cup under the back into which both channels lead.

Tangent line/arc chains of the outlines are built as one exact rational (degree 2)
B-spline each, so that every smooth wall is a single face.
"""
import math

import cadquery as cq
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge
from OCP.Geom import Geom_BSplineCurve
from OCP.gp import gp_Pnt
from OCP.TColgp import TColgp_Array1OfPnt
from OCP.TColStd import TColStd_Array1OfInteger, TColStd_Array1OfReal

# ---------------- driving dimensions (mm) ----------------
W_FRONT = 100.0      # width at the front (slot) face
DEPTH = 124.8        # front face to back apex
HEIGHT = 47.0        # overall thickness
SIDE_SLOPE = 0.0964  # inward taper of the sides (dx/dy)
BACK_R = 53.1        # radius of the back arc
CORNER_R = 15.4      # blend radius between tapered sides and back arc

SLOT_W = 30.0        # U-slot width
SLOT_DEPTH = 66.4    # front face to end of slot

HOLE_D = 4.2         # small through holes from the top
HOLE_X = 35.3
HOLE_Y1 = 29.4
HOLE_Y2 = 99.9
CEN_HOLE_D = 4.2     # blind drilled hole on the centre line
CEN_HOLE_Y = 77.9
CEN_HOLE_DEPTH = 14.0
CEN_HOLE_TIP = 60.0  # included angle of the drill point at the bottom of the blind hole

# underside features
POCKET_D = 8.0       # depth of the front pockets and of the wiring channels
LIP_W = 8.0          # outer lip left at the front of each prong
POCKET_BACK = 25.0   # y where the front pockets end
POCKET_R = 4.5       # inside corner radius of the front pockets
BOSS_X = 30.4        # screw bosses in the front pockets
BOSS_Y = 13.8
BOSS_D = 7.5
BOSS_CHAMFER = 1.2
BOSS_HOLE_D = 3.0
BOSS_HOLE_DEPTH = 10.0
WALL_T = 4.0         # wall left between slot and channel
CH_W = 8.0           # channel width
CH_END = 107.2       # y where the channels end
CH_END_R = 2.0       # corner radius at the closed end of each channel
LINK_W = 12.4        # width of the cross passage joining both channels through the cup
RELIEF = 0.5         # the island between the channels (walls round the slot) sits this far up
CUP_Y = 99.4         # ball-end cup under the back
CUP_R = 17.0
TIP_LAND = 0.3       # tiny flat at the drill point / cup crown (avoids degenerate apexes)

EPS = 0.001
hw = W_FRONT / 2.0


# ---------------- helpers ----------------
def chain_edge(segs):
    """One exact rational quadratic B-spline through a G1 chain of segments.

    segs: ("L", p0, p1) straight line, or ("A", centre, radius, a0, a1) circular arc
    from angle a0 to a1 (radians).  Each line becomes one Bezier piece, each arc one
    rational piece per <= 90 degrees, so the curve is exactly the line/arc chain.
    """
    pieces = []
    for s in segs:
        if s[0] == "L":
            p0, p1 = s[1], s[2]
            pm = ((p0[0] + p1[0]) / 2.0, (p0[1] + p1[1]) / 2.0)
            pieces.append([(p0, 1.0), (pm, 1.0), (p1, 1.0)])
        else:
            _, c, r, a0, a1 = s
            n = max(1, int(math.ceil(abs(a1 - a0) / (math.pi / 2) - 1e-9)))
            for i in range(n):
                t0 = a0 + (a1 - a0) * i / n
                t1 = a0 + (a1 - a0) * (i + 1) / n
                h = (t1 - t0) / 2.0
                tm = (t0 + t1) / 2.0
                p0 = (c[0] + r * math.cos(t0), c[1] + r * math.sin(t0))
                p2 = (c[0] + r * math.cos(t1), c[1] + r * math.sin(t1))
                rm = r / math.cos(h)
                pm = (c[0] + rm * math.cos(tm), c[1] + rm * math.sin(tm))
                pieces.append([(p0, 1.0), (pm, math.cos(h)), (p2, 1.0)])
    poles = [pieces[0][0]]
    for pc in pieces:
        poles += [pc[1], pc[2]]
    npc = len(pieces)
    arr_p = TColgp_Array1OfPnt(1, len(poles))
    arr_w = TColStd_Array1OfReal(1, len(poles))
    for i, (p, w) in enumerate(poles):
        arr_p.SetValue(i + 1, gp_Pnt(p[0], p[1], 0.0))
        arr_w.SetValue(i + 1, w)
    arr_k = TColStd_Array1OfReal(1, npc + 1)
    arr_m = TColStd_Array1OfInteger(1, npc + 1)
    for i in range(npc + 1):
        arr_k.SetValue(i + 1, float(i))
        arr_m.SetValue(i + 1, 3 if i in (0, npc) else 2)
    curve = Geom_BSplineCurve(arr_p, arr_w, arr_k, arr_m, 2)
    return cq.Edge(BRepBuilderAPI_MakeEdge(curve).Edge())


def line_edge(p0, p1):
    return cq.Edge.makeLine(cq.Vector(p0[0], p0[1], 0), cq.Vector(p1[0], p1[1], 0))


def prism(edges, z0, h):
    """Closed planar profile (list of edges at z=0) extruded from z0 by h."""
    wire = cq.Wire.assembleEdges(edges)
    face = cq.Face.makeFromWires(wire)
    return cq.Solid.extrudeLinear(face, cq.Vector(0, 0, h)).translate(cq.Vector(0, 0, z0))


# ---------------- outline: tapered sides, filleted back arc ----------------
k = SIDE_SLOPE
yc = DEPTH - BACK_R                       # centre of the back arc
nk = math.hypot(1.0, k)
# right-hand fillet centre: r inside the side line x = hw - k*y, (R - r) from (0, yc)
a_ = k * k + 1
b_ = -2 * k * (hw - CORNER_R * nk) - 2 * yc
c_ = (hw - CORNER_R * nk) ** 2 + yc * yc - (BACK_R - CORNER_R) ** 2
fy = (-b_ + math.sqrt(b_ * b_ - 4 * a_ * c_)) / (2 * a_)
fx = hw - k * fy - CORNER_R * nk
t_side = (fx + CORNER_R / nk, fy + CORNER_R * k / nk)   # fillet meets side
ang_side = math.atan2(k, 1.0)                          # outward normal of the side
ang_arc = math.atan2(fy - yc, fx)                      # direction centre -> fillet

outline = chain_edge(
    [
        ("L", (hw, 0.0), t_side),
        ("A", (fx, fy), CORNER_R, ang_side, ang_arc),
        ("A", (0.0, yc), BACK_R, ang_arc, math.pi - ang_arc),
        ("A", (-fx, fy), CORNER_R, math.pi - ang_arc, math.pi - ang_side),
        ("L", (-t_side[0], t_side[1]), (-hw, 0.0)),
    ]
)
body = cq.Workplane("XY").add(prism([outline, line_edge((-hw, 0.0), (hw, 0.0))], 0.0, HEIGHT))

# ---------------- U slot ----------------
sr = SLOT_W / 2.0
sy = SLOT_DEPTH - sr
slot_edge = chain_edge(
    [
        ("L", (-sr, -1.0), (-sr, sy)),
        ("A", (0.0, sy), sr, math.pi, 0.0),
        ("L", (sr, sy), (sr, -1.0)),
    ]
)
body = body.cut(prism([slot_edge, line_edge((sr, -1.0), (-sr, -1.0))], -1.0, HEIGHT + 2))

# ---------------- top holes ----------------
holes = (
    cq.Workplane("XY")
    .pushPoints([(x, y) for x in (-HOLE_X, HOLE_X) for y in (HOLE_Y1, HOLE_Y2)])
    .circle(HOLE_D / 2)
    .extrude(HEIGHT + 2)
    .translate((0, 0, -1))
)
body = body.cut(holes)

# blind centre hole ending in a drill point (tip angle CEN_HOLE_TIP)
tip = (CEN_HOLE_D / 2 - TIP_LAND / 2) / math.tan(math.radians(CEN_HOLE_TIP / 2))
cen = (
    cq.Workplane("XZ")
    .polyline(
        [
            (0, HEIGHT + 1),
            (CEN_HOLE_D / 2, HEIGHT + 1),
            (CEN_HOLE_D / 2, HEIGHT - CEN_HOLE_DEPTH),
            (TIP_LAND / 2, HEIGHT - CEN_HOLE_DEPTH - tip),
            (0, HEIGHT - CEN_HOLE_DEPTH - tip),
        ]
    )
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .translate((0, CEN_HOLE_Y, 0))
)
body = body.cut(cen)

# ---------------- underside ----------------
x_in = SLOT_W / 2.0
x_out = hw - LIP_W
x0 = x_in + WALL_T                      # inner edge of the channel
for sgn in (-1, 1):
    # front pocket, open to the front face and to the slot, rounded outer corner
    pr = POCKET_R
    pk_chain = chain_edge(
        [
            ("L", (sgn * x_out, -1.0), (sgn * x_out, POCKET_BACK - pr)),
            (
                "A",
                (sgn * (x_out - pr), POCKET_BACK - pr),
                pr,
                0.0 if sgn > 0 else math.pi,
                math.pi / 2,
            ),
            ("L", (sgn * (x_out - pr), POCKET_BACK), (sgn * x_in, POCKET_BACK)),
        ]
    )
    pocket = prism(
        [
            pk_chain,
            line_edge((sgn * x_in, POCKET_BACK), (sgn * x_in, -1.0)),
            line_edge((sgn * x_in, -1.0), (sgn * x_out, -1.0)),
        ],
        -EPS,
        POCKET_D,
    )
    body = body.cut(pocket)

    # screw boss (chamfered end) with a blind hole
    boss = (
        cq.Workplane("XY")
        .center(sgn * BOSS_X, BOSS_Y)
        .circle(BOSS_D / 2)
        .extrude(POCKET_D + 0.5)
        .faces("<Z")
        .edges()
        .chamfer(BOSS_CHAMFER)
    )
    body = body.union(boss)
    bh = (
        cq.Workplane("XY")
        .center(sgn * BOSS_X, BOSS_Y)
        .circle(BOSS_HOLE_D / 2)
        .extrude(BOSS_HOLE_DEPTH)
        .translate((0, 0, -0.01))
    )
    body = body.cut(bh)

    # wiring channel along the prong (closed back end with rounded corners)
    xl, xr = sorted((sgn * x0, sgn * (x0 + CH_W)))
    y0, rc = POCKET_BACK - 1.0, CH_END_R
    ch_chain = chain_edge(
        [
            ("L", (xl, y0), (xl, CH_END - rc)),
            ("A", (xl + rc, CH_END - rc), rc, math.pi, math.pi / 2),
            ("L", (xl + rc, CH_END), (xr - rc, CH_END)),
            ("A", (xr - rc, CH_END - rc), rc, math.pi / 2, 0.0),
            ("L", (xr, CH_END - rc), (xr, y0)),
        ]
    )
    body = body.cut(prism([ch_chain, line_edge((xr, y0), (xl, y0))], -EPS, POCKET_D))

# cross passage joining both channels through the cup
link = (
    cq.Workplane("XY")
    .center(0, CUP_Y)
    .rect(2 * x0 + 1.0, LINK_W)
    .extrude(POCKET_D)
    .translate((0, 0, -EPS))
)
body = body.cut(link)

# shallow relief of the island enclosed by the slot, the channels and the cross passage
relief = (
    cq.Workplane("XY")
    .center(0, (POCKET_BACK - 1 + CUP_Y - LINK_W / 2) / 2)
    .rect(2 * x0, CUP_Y - LINK_W / 2 - POCKET_BACK + 1)
    .extrude(RELIEF)
    .translate((0, 0, -EPS))
)
body = body.cut(relief)

# ball-end cup under the back (crown flattened to a tiny land: no degenerate pole)
ztop = math.sqrt(CUP_R ** 2 - TIP_LAND ** 2)
cup = (
    cq.Workplane("XZ")
    .moveTo(0, -1)
    .lineTo(CUP_R, -1)
    .lineTo(CUP_R, 0)
    .radiusArc((TIP_LAND, ztop), -CUP_R)
    .lineTo(0, ztop)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .translate((0, CUP_Y, 0))
)
body = body.cut(cup)

# centre the part on its bounding box in Y
result = body.translate((0, -DEPTH / 2, 0))

VIEW = {"azimuth": 45, "elevation": 26}
